import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L_CC = 150.0        # centre distance between the two end bores
W = 20.0            # bar width (Y)
R_END = W / 2.0     # radius of rounded ends
H = 20.0            # full body height (Z)
H_LUG = 10.0        # height of the thin lug at the +X end
WALL = 3.0          # side wall thickness around the truss pockets
RIB = 2.7           # diagonal rib thickness
NODE_Y = 7.56       # |y| of truss nodes
X_TRUSS_A = 12.2    # first truss node / left edge of pocket 1
X_TRUSS_B = 125.6   # last truss node / right edge of pocket 4
POCKET_R = 0.6      # corner radius of the pockets
X_TIP = 147.2       # sharp tips of the V-notched end of the full-height body
X_V = 130.2         # apex of the V notch
V_TIP_R = 0.46      # round on the two V arm tips
D_HOLE_L = 13.1     # bore at the splined end
D_HOLE_R = 15.0     # bore in the lug
CHAMFER_BOT = 1.5   # chamfer round the bottom outline
N_TEETH = 18        # radial face-spline teeth
TOOTH_ANG = 7.7     # angular width of one tooth (deg)
TOOTH_H = 0.85
TOOTH_PHASE = 0.5      # teeth offset by half a pitch (gap on the X axis)
HOLE_CHAMFER = 0.5

# ---------------- base outline (full stadium, lug height) ----------------
base = (
    cq.Workplane("XY")
    .center(L_CC / 2.0, 0)
    .slot2D(L_CC + 2 * R_END, W)
    .extrude(H_LUG)
)

# ---------------- full-height body with V-notched end ----------------
hy = W / 2.0
upper = (
    cq.Workplane("XY")
    .moveTo(0, -hy)
    .lineTo(X_TIP, -hy)
    .lineTo(X_V, 0)
    .lineTo(X_TIP, hy)
    .lineTo(0, hy)
    .threePointArc((-R_END, 0), (0, -hy))
    .close()
    .extrude(H)
)
# round the two sharp arm tips of the V notch
upper = upper.edges("|Z").edges(
    cq.selectors.BoxSelector((X_TIP - 0.2, -hy - 1, -1), (X_TIP + 0.2, hy + 1, H + 1))
).fillet(V_TIP_R)

body = base.union(upper).clean()
body = body.faces("<Z").edges().chamfer(CHAMFER_BOT)

# ---------------- bores (with a small chamfer at the bottom edge) ----------------
def bore(xc, dia):
    r = dia / 2.0
    cyl = cq.Workplane("XY").center(xc, 0).circle(r).extrude(H + 5).translate((0, 0, -1))
    cone = cq.Solid.makeCone(
        r + HOLE_CHAMFER + 1.0, r, HOLE_CHAMFER + 1.0,
        cq.Vector(xc, 0, -1.0), cq.Vector(0, 0, 1)
    )
    return cyl.union(cq.Workplane("XY").add(cone))


body = body.cut(bore(0.0, D_HOLE_L))
body = body.cut(bore(L_CC, D_HOLE_R))


# ---------------- truss pockets ----------------
def clip(poly, a, b, c):
    """keep the part of polygon where a*x + b*y <= c"""
    out = []
    n = len(poly)
    for i in range(n):
        p = poly[i]
        q = poly[(i + 1) % n]
        fp = a * p[0] + b * p[1] - c
        fq = a * q[0] + b * q[1] - c
        if fp <= 0:
            out.append(p)
        if (fp < 0 < fq) or (fq < 0 < fp):
            t = fp / (fp - fq)
            out.append((p[0] + t * (q[0] - p[0]), p[1] + t * (q[1] - p[1])))
    return out


def line_halfplane(p0, p1, offset, side_pt):
    """half plane bounded by line p0-p1 shifted by 'offset' towards side_pt"""
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    ln = math.hypot(dx, dy)
    nx, ny = -dy / ln, dx / ln
    # orient normal so that side_pt lies on the positive side
    if nx * (side_pt[0] - p0[0]) + ny * (side_pt[1] - p0[1]) < 0:
        nx, ny = -nx, -ny
    # region: n.(x - p0) >= offset  ->  -n.x <= -(n.p0 + offset)
    return (-nx, -ny, -(nx * p0[0] + ny * p0[1] + offset))


hi = hy - WALL
d = (X_TRUSS_B - X_TRUSS_A) / 3.0
nodes = [
    (X_TRUSS_A, -NODE_Y),
    (X_TRUSS_A + d, NODE_Y),
    (X_TRUSS_A + 2 * d, -NODE_Y),
    (X_TRUSS_B, NODE_Y),
]
big = [(X_TRUSS_A - 50, -hi), (X_TRUSS_B + 50, -hi), (X_TRUSS_B + 50, hi), (X_TRUSS_A - 50, hi)]
ht = RIB / 2.0

pockets = []
# pocket 1 : left of rib 0, right of x = A
p = clip(big, -1, 0, -X_TRUSS_A)
p = clip(p, *line_halfplane(nodes[0], nodes[1], ht, (X_TRUSS_A, hi)))
pockets.append(p)
# pocket 2 : below ribs 0 and 1
p = clip(big, *line_halfplane(nodes[0], nodes[1], ht, (nodes[1][0], -hi)))
p = clip(p, *line_halfplane(nodes[1], nodes[2], ht, (nodes[1][0], -hi)))
pockets.append(p)
# pocket 3 : above ribs 1 and 2
p = clip(big, *line_halfplane(nodes[1], nodes[2], ht, (nodes[2][0], hi)))
p = clip(p, *line_halfplane(nodes[2], nodes[3], ht, (nodes[2][0], hi)))
pockets.append(p)
# pocket 4 : right of rib 2, left of x = B
p = clip(big, 1, 0, X_TRUSS_B)
p = clip(p, *line_halfplane(nodes[2], nodes[3], ht, (X_TRUSS_B, -hi)))
pockets.append(p)

for poly in pockets:
    prism = (
        cq.Workplane("XY")
        .polyline(poly)
        .close()
        .extrude(H + 4)
        .translate((0, 0, -2))
    )
    try:
        prism = prism.edges("|Z").fillet(POCKET_R)
    except Exception:
        pass
    body = body.cut(prism)

# ---------------- radial face-spline teeth on the left boss ----------------
# sector shaped teeth (constant angular width, radial flanks), trimmed by the
# bore and by the end radius
r_in = D_HOLE_L / 2.0
r0, r1 = r_in - 1.0, R_END + 1.0
half = math.radians(TOOTH_ANG) / 2.0
teeth = None
for i in range(N_TEETH):
    a = math.radians(360.0 * (i + TOOTH_PHASE) / N_TEETH)
    pts = [
        (r0 * math.cos(a - half), r0 * math.sin(a - half)),
        (r1 * math.cos(a - half), r1 * math.sin(a - half)),
        (r1 * math.cos(a + half), r1 * math.sin(a + half)),
        (r0 * math.cos(a + half), r0 * math.sin(a + half)),
    ]
    t_i = cq.Workplane("XY").workplane(offset=H).polyline(pts).close().extrude(TOOTH_H)
    teeth = t_i if teeth is None else teeth.union(t_i)
ring = (
    cq.Workplane("XY")
    .circle(R_END)
    .circle(r_in)
    .extrude(TOOTH_H + 1)
    .translate((0, 0, H - 0.5))
)
teeth = teeth.intersect(ring)
body = body.union(teeth)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
